import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Curved guard / cover bracket (moulded part)
#   X : towards the bulge of the cover
#   Y : along the cover (axis of the curved surfaces)
#   Z : up  (mounting bar with two vertical holes on top)
# Features: mounting bar + top plate, curved cover (upper bend + large arc),
# front wing with hanging leg and slot, bevelled front edge of the cover,
# thick C-shaped rib with two holes at the rear end, hinge eye + latch below.
# ---------------------------------------------------------------------------

# ---- overall ----------------------------------------------------------------
Z_TOP = 238.0          # top of mounting bar / cover
Y_END = 202.0          # +Y end of the cover
WALL = 11.0            # wall thickness of the cover sheet

# ---- cover profile (XZ), all surfaces are extrusions along Y -----------------
C2 = (-47.3, 118.5)    # centre of the large outer arc
R2O = 158.6            # radius of the large outer arc
ALPHA_T = math.radians(25.6)   # where the upper bend blends into the large arc
R1O = 101.0            # outer radius of the upper bend
R1I = R1O - WALL       # inner radius of the upper bend
C1 = (C2[0] + (R2O - R1O) * math.cos(ALPHA_T),     # upper bend is tangent
      C2[1] + (R2O - R1O) * math.sin(ALPHA_T))     # inside the large arc

Z_SHELL_BOT = 46.0     # lower end of the cover
X_IN_BOT = 82.0        # inner face at the lower end
IN_MID = (96.5, 116.0)  # inner face at mid height
Z_FLAT = 75.0          # below this the outer face continues along the tangent (straight)
LOWER_STATIONS = (160.0, 135.0, 118.5, 100.0, 75.0, 60.0)

# ---- top plate & mounting bar -------------------------------------------------
Z_PLATE_BOT = 221.5
X_LIP0 = 36.6          # flat top of the plate ends here ...
X_LIP1 = 44.4          # ... and a short bevel lands on the bend here
BAR_W = 22.0           # bar width (X)
Z_BAR_BOT = 214.0
BAR_FILLET = 3.0
Y_BODY0 = 82.0         # -Y end of the main body (top plate)
Y_BAR0 = 92.6          # -Y end of the mounting bar
X_NOTCH = 31.5
R_NOTCH = 9.0
BAR_HOLE_X = 8.75
BAR_HOLE_YS = (117.5, 177.2)
BAR_HOLE_R = 7.3

# ---- front wing with hanging leg ------------------------------------------------
Y_WING0 = 0.0
Z_LEG_BOT = 113.0
Y_LEG1 = 49.7          # leg width (Y)
SLOT_Y1 = 88.0         # slot between leg and cover
SLOT_TOP = 196.5
SLOT_R = 9.4
WING_INSET = 1.0       # wing surface slightly below the cover surface (visible seam)
LEG_R = 4.5            # rounding of the leg's lower end
WING_END_DEG = 68.0    # angular position of the rounded upper end of the wing

# ---- bevelled front end of the lower cover -------------------------------------
TAPER_Y1 = 122.0            # bevel runs out on the cover here
TAPER_CLEAR = 0.4           # (construction) rear cutter section clearance
TAPER_OVER = 1.5            # (construction) rear cutter section overshoot in Y
TAPER_LOW = (97.0, 75.0)    # front edge of the bevel low down
TAPER_MID = (97.5, 116.0)   # front edge of the bevel at mid height
TAPER_TOP_X = 85.5          # front edge of the bevel just below the bend

# ---- inner C-rib at the +Y end ----------------------------------------------------
RIB_T = 27.5
RIB_HOLES = [(57.5, 197.0), (57.2, 114.3)]
RIB_HOLE_R = 7.0
NOTCH_MID = (89.0, 155.0)   # deepest point of the concave notch between the lobes

# ---- hinge eye and latch at the bottom ------------------------------------------
HINGE_X = (85.7, 111.0)
HINGE_Y = (132.0, 167.0)
HINGE_Z = (0.8, 47.0)
HINGE_R_TR = 14.0      # profile roundings of the hinge eye
HINGE_R_BR = 9.0
HINGE_R_BL = 3.0
HINGE_EDGE_R = 2.5
HINGE_Z_STEP = 17.0    # the eye is wider (towards -X) above this height
HINGE_HOLE = (99.4, 28.4)
HINGE_HOLE_R = 6.7
LATCH_X = (77.0, 99.4)
LATCH_Y = (91.4, 132.5)
LATCH_Z = (17.0, 47.0)
LATCH_CH = 5.0

XB = 140.0             # helper: far outside the part in +X


# ---------------------------------------------------------------------------
def pol(c, r, a):
    return (c[0] + r * math.cos(a), c[1] + r * math.sin(a))


def ang(c, p):
    return math.atan2(p[1] - c[1], p[0] - c[0])


def mid_arc(c, r, a0, a1):
    return pol(c, r, 0.5 * (a0 + a1))


def arc_x(c, r, z):
    return c[0] + math.sqrt(r ** 2 - (z - c[1]) ** 2)


def xz_wp(y1):
    """Workplane in the XZ plane located at Y = y1; extrude(+d) goes to -Y."""
    return cq.Workplane("XZ", origin=(0, y1, 0))


# key points of the profile
a_lip = math.acos((X_LIP1 - C1[0]) / R1O)
P_LIP = pol(C1, R1O, a_lip)                 # bevel lands on the bend
P_TAN_O = pol(C1, R1O, ALPHA_T)             # outer tangent point bend / large arc
P_TAN_I = pol(C1, R1I, ALPHA_T)             # inner tangent point
P_J = (arc_x(C2, R2O, Z_FLAT), Z_FLAT)      # large arc ends here, tangent line below
a_j = ang(C2, P_J)
X_BOT_O = P_J[0] + math.tan(a_j) * (Z_FLAT - Z_SHELL_BOT)   # outer face at the lower end


def lower_outer_x(z):
    """large arc above Z_FLAT, its tangent line below."""
    if z >= Z_FLAT:
        return arc_x(C2, R2O, z)
    return P_J[0] + math.tan(a_j) * (Z_FLAT - z)


# the lower cover face is one smooth curve through these stations (top -> bottom)
LOWER_PTS = [P_TAN_O] + [(lower_outer_x(z), z) for z in LOWER_STATIONS] + [(X_BOT_O, Z_SHELL_BOT)]
T_TOP = (math.sin(ALPHA_T), -math.cos(ALPHA_T))
T_BOT = (math.sin(a_j), -math.cos(a_j))
a_pb = math.asin((Z_PLATE_BOT - C1[1]) / R1I)
P_PB = pol(C1, R1I, a_pb)


def outer_chain(wp):
    """flat top -> bevel -> upper bend -> large arc (ends at the bottom)."""
    return (wp.moveTo(0, Z_TOP)
            .lineTo(X_LIP0, Z_TOP)
            .lineTo(*P_LIP)
            .threePointArc(mid_arc(C1, R1O, a_lip, ALPHA_T), P_TAN_O)
            .spline(LOWER_PTS[1:], tangents=[T_TOP, T_BOT], includeCurrent=True))


# ---------------------------------------------------------------------------
# main body: top plate + cover, Y_BODY0 .. Y_END
body = (
    outer_chain(xz_wp(Y_END))
    .lineTo(X_IN_BOT, Z_SHELL_BOT)
    .threePointArc(IN_MID, P_TAN_I)
    .threePointArc(mid_arc(C1, R1I, ALPHA_T, a_pb), P_PB)
    .lineTo(BAR_W, Z_PLATE_BOT)
    .lineTo(BAR_W, Z_BAR_BOT)
    .lineTo(0, Z_BAR_BOT)
    .close()
    .extrude(Y_END - Y_BODY0)
)

# round the lower edges of the mounting bar
body = body.edges(cq.selectors.BoxSelector((-1, Y_BODY0 - 1, Z_BAR_BOT - 1),
                                            (1, Y_END + 1, Z_BAR_BOT + 1))).fillet(BAR_FILLET)

# recess of the bar at its -Y end (rounded inside corner)
c45 = math.cos(math.radians(45))
notch = (
    cq.Workplane("XY", origin=(0, 0, 200))
    .moveTo(-5, 60)
    .lineTo(X_NOTCH, 60)
    .lineTo(X_NOTCH, Y_BAR0 - R_NOTCH)
    .threePointArc((X_NOTCH - R_NOTCH + R_NOTCH * c45, Y_BAR0 - R_NOTCH + R_NOTCH * c45),
                   (X_NOTCH - R_NOTCH, Y_BAR0))
    .lineTo(-5, Y_BAR0)
    .close()
    .extrude(50)
)
body = body.cut(notch)

# ---------------------------------------------------------------------------
# front wing: bent strip following the upper bend, ending in a vertical leg
WO = R1O - WING_INSET
WI = R1I - WING_INSET
a_we = math.radians(WING_END_DEG)
cap_c = pol(C1, 0.5 * (WO + WI), a_we)
cap_tip = (cap_c[0] - 0.5 * WALL * math.sin(a_we), cap_c[1] + 0.5 * WALL * math.cos(a_we))
P_WT = pol(C1, WO, ALPHA_T)
X_LEG_O = P_WT[0]
X_LEG_I = X_LEG_O - WALL
a_li = math.acos((X_LEG_I - C1[0]) / WI)
wing = (
    xz_wp(Y_BODY0 + 0.5)
    .moveTo(*pol(C1, WO, a_we))
    .threePointArc(mid_arc(C1, WO, a_we, ALPHA_T), P_WT)
    .lineTo(X_LEG_O, Z_LEG_BOT)
    .lineTo(X_LEG_I, Z_LEG_BOT)
    .lineTo(X_LEG_I, C1[1] + WI * math.sin(a_li))
    .threePointArc(mid_arc(C1, WI, a_li, a_we), pol(C1, WI, a_we))
    .threePointArc(cap_tip, pol(C1, WO, a_we))
    .close()
    .extrude(Y_BODY0 + 0.5 - Y_WING0)
)
# rounded lower end of the leg
wing = wing.edges(cq.selectors.BoxSelector((X_LEG_I - 1, -1, Z_LEG_BOT - 1),
                                            (X_LEG_O + 1, Y_BODY0 + 1, Z_LEG_BOT + 1))).fillet(LEG_R)

part = body.union(wing)

# ---------------------------------------------------------------------------
# bevelled front end of the lower cover: ruled surface from a thin front edge
# (at the slot) to the full cover surface at TAPER_Y1; full wall at the foot


def taper_section(y, front):
    wp = cq.Workplane("XZ", origin=(0, y, 0))
    if front:
        p0 = (X_BOT_O - TAPER_CLEAR, Z_SHELL_BOT - 1.5)
        p1 = (X_BOT_O - TAPER_CLEAR, Z_SHELL_BOT)
        pts = [TAPER_LOW, TAPER_MID, (TAPER_TOP_X, P_TAN_O[1])]
        wp = wp.moveTo(*p0).lineTo(*p1).spline(pts, includeCurrent=True)
    else:
        # rear section sits just outside the cover face, so the bevel runs out cleanly
        p0 = (X_BOT_O + TAPER_CLEAR, Z_SHELL_BOT - 1.5)
        p1 = (X_BOT_O + TAPER_CLEAR, Z_SHELL_BOT)
        pts = [(x + TAPER_CLEAR, z) for (x, z) in reversed(LOWER_PTS)][1:]
        wp = wp.moveTo(*p0).lineTo(*p1).spline(pts, tangents=[(-T_BOT[0], -T_BOT[1]),
                                                              (-T_TOP[0], -T_TOP[1])],
                                               includeCurrent=True)
    return wp.lineTo(XB, P_TAN_O[1]).lineTo(XB, p0[1]).close()


w_a = taper_section(SLOT_Y1 - 0.01, True).wires().val()
w_b = taper_section(TAPER_Y1 + TAPER_OVER, False).wires().val()
taper_cut = cq.Workplane("XY").add(cq.Solid.makeLoft([w_a, w_b], True))
part = part.cut(taper_cut)

# ---------------------------------------------------------------------------
# slot between the leg and the cover (rounded top corners)
slot = (
    cq.Workplane("YZ", origin=(60, 0, 0))
    .moveTo(Y_LEG1, -10)
    .lineTo(SLOT_Y1, -10)
    .lineTo(SLOT_Y1, SLOT_TOP - SLOT_R)
    .threePointArc((SLOT_Y1 - SLOT_R + SLOT_R * c45, SLOT_TOP - SLOT_R + SLOT_R * c45),
                   (SLOT_Y1 - SLOT_R, SLOT_TOP))
    .lineTo(Y_LEG1 + SLOT_R, SLOT_TOP)
    .threePointArc((Y_LEG1 + SLOT_R - SLOT_R * c45, SLOT_TOP - SLOT_R + SLOT_R * c45),
                   (Y_LEG1, SLOT_TOP - SLOT_R))
    .close()
    .extrude(80)
)
part = part.cut(slot)

# ---------------------------------------------------------------------------
# inner C-shaped rib at the +Y end, with two through holes along Y
outer_region = (
    outer_chain(xz_wp(Y_END))
    .lineTo(0, Z_SHELL_BOT)
    .close()
    .extrude(RIB_T)
)
rib = (
    xz_wp(Y_END)
    .moveTo(45.2, 226.0)
    .lineTo(45.2, 194.0)
    .lineTo(57.5, 178.6)
    .lineTo(74.5, 178.6)
    .threePointArc(NOTCH_MID, (79.0, 132.5))
    .lineTo(58.3, 132.5)
    .lineTo(44.5, 117.1)
    .lineTo(44.5, 98.6)
    .lineTo(62.0, 81.0)
    .lineTo(X_IN_BOT, Z_SHELL_BOT)
    .lineTo(XB, Z_SHELL_BOT)
    .lineTo(XB, 226.0)
    .close()
    .extrude(RIB_T)
)
rib = rib.intersect(outer_region)
for (hx, hz) in RIB_HOLES:
    rib = rib.cut(
        cq.Workplane("XZ", origin=(0, Y_END + 1, 0)).center(hx, hz).circle(RIB_HOLE_R).extrude(RIB_T + 2)
    )
part = part.union(rib)

# vertical holes in the mounting bar
for hy in BAR_HOLE_YS:
    part = part.cut(
        cq.Workplane("XY", origin=(BAR_HOLE_X, hy, Z_BAR_BOT - 5)).circle(BAR_HOLE_R).extrude(40)
    )

# ---------------------------------------------------------------------------
# hinge eye + latch at the lower end
HX0, HX1 = HINGE_X
HZ0, HZ1 = HINGE_Z
hinge = (
    xz_wp(HINGE_Y[1])
    .moveTo(LATCH_X[0], HZ1)
    .lineTo(HX1 - HINGE_R_TR, HZ1)
    .threePointArc((HX1 - HINGE_R_TR + HINGE_R_TR * c45, HZ1 - HINGE_R_TR + HINGE_R_TR * c45),
                   (HX1, HZ1 - HINGE_R_TR))
    .lineTo(HX1, HZ0 + HINGE_R_BR)
    .threePointArc((HX1 - HINGE_R_BR + HINGE_R_BR * c45, HZ0 + HINGE_R_BR - HINGE_R_BR * c45),
                   (HX1 - HINGE_R_BR, HZ0))
    .lineTo(HX0 + HINGE_R_BL, HZ0)
    .threePointArc((HX0 + HINGE_R_BL - HINGE_R_BL * c45, HZ0 + HINGE_R_BL - HINGE_R_BL * c45),
                   (HX0, HZ0 + HINGE_R_BL))
    .lineTo(HX0, HINGE_Z_STEP)
    .lineTo(LATCH_X[0], HINGE_Z_STEP)
    .close()
    .extrude(HINGE_Y[1] - HINGE_Y[0])
)
for yy in HINGE_Y:
    try:
        hinge = hinge.edges(cq.selectors.BoxSelector((HX0 + 0.5, yy - 1, HZ0 - 1),
                                                      (HX1 + 1, yy + 1, HZ1 - 0.5))).fillet(HINGE_EDGE_R)
    except Exception:
        pass

latch = (
    cq.Workplane("XY")
    .box(LATCH_X[1] - LATCH_X[0], LATCH_Y[1] - LATCH_Y[0], LATCH_Z[1] - LATCH_Z[0], centered=False)
    .translate((LATCH_X[0], LATCH_Y[0], LATCH_Z[0]))
)
latch = latch.faces("<Y").edges("|Z").chamfer(LATCH_CH)
latch = latch.faces("<Y").edges(">Z").chamfer(LATCH_CH)

part = part.union(hinge).union(latch)

# pin bore through the eye, continuing as an open groove along the latch
part = part.cut(
    cq.Workplane("XZ", origin=(0, HINGE_Y[1] + 1, 0)).center(*HINGE_HOLE).circle(HINGE_HOLE_R)
    .extrude(HINGE_Y[1] - LATCH_Y[0] + 2)
)

result = part
